"""Segmented internal-toothed ring (14 rack segments) with four radial
mounting arms.  Each segment: annular sector with trapezoid/round-root teeth
on the inner edge, a tongue on its counter-clockwise end, a groove on its
clockwise end and a small locating hole; four segments carry a radial arm
with a rounded, drilled end."""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 200.0          # outer radius of the segmented ring
R_ROOT = 181.7         # tooth root radius (inner toothed edge)
R_TIP = 175.8          # tooth tip radius
THK = 5.0              # plate thickness

N_SEG = 14             # number of ring segments
SEG_PITCH = 360.0 / N_SEG
SEG_GAP = 2.45         # angular gap between neighbouring segments (deg)
SEG_PHASE = -0.23      # small clockwise clocking of the whole segment set (deg)

TEETH_PER_SEG = 11
TOOTH_PITCH = SEG_PITCH / TEETH_PER_SEG        # deg
TOOTH_HALF_ANGLE = 20.0   # flank angle to the tooth-space centre line (deg)
ROOT_RAD = 1.3             # full root radius of each tooth space
TIP_FILLET = 0.7          # rounding of the tooth tip corners

HOLE_R_POS = 191.0     # radius of the locating hole in every segment
HOLE_D = 2.4

# tongue (counter-clockwise end) / groove (clockwise end)
TONGUE_R1 = 186.5
TONGUE_R2 = 196.0
TONGUE_LEN = 3.0
GROOVE_DEPTH = 2.2
GROOVE_CLR = 0.2

# radial arms on four segments, at +/-ARM_SPLAY from the +/-Y axis
ARM_SEG_IDX = (3, 4, 10, 11)   # segments centred at 77.1, 102.9, 257.1, 282.9 deg
ARM_SPLAY = 15.0       # deg from the +/-Y axis -> arms at 75, 105, 255, 285 deg
ARM_W = 18.0
ARM_END_R = 243.0      # radius of the arm end hole / rounded-end centre
ARM_HOLE_D = 2.4


def pol(r, a_deg):
    a = math.radians(a_deg)
    return (r * math.cos(a), r * math.sin(a))


def sector(r1, r2, a1, a2, h):
    am = 0.5 * (a1 + a2)
    return (
        cq.Workplane("XY")
        .moveTo(*pol(r1, a1))
        .lineTo(*pol(r2, a1))
        .threePointArc(pol(r2, am), pol(r2, a2))
        .lineTo(*pol(r1, a2))
        .threePointArc(pol(r1, am), pol(r1, a1))
        .close()
        .extrude(h)
    )


def local_box(a_deg, r1, r2, t1, t2, z1, z2):
    """Box whose radial span is r1..r2 along direction a_deg and whose
    tangential span is t1..t2 (mm, measured along the CCW tangent)."""
    a = math.radians(a_deg)
    er = (math.cos(a), math.sin(a))
    et = (-math.sin(a), math.cos(a))

    def p(r, t):
        return (r * er[0] + t * et[0], r * er[1] + t * et[1])

    return (
        cq.Workplane("XY")
        .workplane(offset=z1)
        .polyline([p(r1, t1), p(r2, t1), p(r2, t2), p(r1, t2)])
        .close()
        .extrude(z2 - z1)
    )


def tooth_gap(a_deg):
    """Tooth space centred on angle a_deg: straight flanks at TOOTH_HALF_ANGLE
    joined by a full root radius whose bottom lies on the root circle."""
    b = math.radians(TOOTH_HALF_ANGLE)
    rr = ROOT_RAD
    uc = R_ROOT - rr                       # root-arc centre (radial coord)
    ua = uc + rr / math.sin(b)             # virtual V apex
    ext = 2.0                              # run flanks past the tip circle
    u_in = R_TIP - ext
    v_in = (ua - u_in) * math.tan(b)
    ut = uc + rr * math.sin(b)             # flank / arc tangent points
    vt = rr * math.cos(b)
    a = math.radians(a_deg)
    er = (math.cos(a), math.sin(a))
    et = (-math.sin(a), math.cos(a))

    def p(u, v):
        return (u * er[0] + v * et[0], u * er[1] + v * et[1])

    return (
        cq.Workplane("XY")
        .workplane(offset=-1)
        .moveTo(*p(u_in, -v_in))
        .lineTo(*p(ut, -vt))
        .threePointArc(p(R_ROOT, 0.0), p(ut, vt))
        .lineTo(*p(u_in, v_in))
        .close()
        .extrude(THK + 2)
    )


def make_segment(arm_tilt=None):
    half = 0.5 * (SEG_PITCH - SEG_GAP)
    seg = sector(R_TIP, R_OUT, -half, half, THK)

    # tooth spaces: a tooth space sits on the segment centre line
    gaps = tooth_gap(0.0)
    j = 1
    while j * TOOTH_PITCH - 0.5 * TOOTH_PITCH < half:
        for sg in (1, -1):
            gaps = gaps.union(tooth_gap(sg * j * TOOTH_PITCH))
        j += 1
    seg = seg.cut(gaps)

    # round the tooth tips: vertical edges lying on the tip circle
    if TIP_FILLET > 0:
        lim = math.radians(half - 0.35 * TOOTH_PITCH)
        tip_edges = []
        for e in seg.edges("|Z").vals():
            c = e.Center()
            r = math.hypot(c.x, c.y)
            if abs(r - R_TIP) < 0.05 and abs(math.atan2(c.y, c.x)) < lim:
                tip_edges.append(e)
        if tip_edges:
            seg = cq.Workplane("XY").newObject([seg.val().fillet(TIP_FILLET, tip_edges)])

    # tongue on the counter-clockwise end
    tongue = local_box(half, TONGUE_R1, TONGUE_R2, -1.0, TONGUE_LEN, 0, THK)
    # groove on the clockwise end
    groove = local_box(-half, TONGUE_R1 - GROOVE_CLR, TONGUE_R2 + GROOVE_CLR,
                       -3.0, GROOVE_DEPTH, -1, THK + 1)
    seg = seg.union(tongue).cut(groove)

    if arm_tilt is not None:
        # radial arm (x along the arm), rotated by arm_tilt about the ring axis
        r0 = R_ROOT + 4.0
        arm = (
            cq.Workplane("XY")
            .center(0.5 * (r0 + ARM_END_R), 0)
            .rect(ARM_END_R - r0, ARM_W)
            .extrude(THK)
            .union(cq.Workplane("XY").center(ARM_END_R, 0).circle(ARM_W / 2).extrude(THK))
            .cut(cq.Workplane("XY").center(ARM_END_R, 0).circle(ARM_HOLE_D / 2)
                 .extrude(THK + 2, both=True))
        )
        arm = arm.rotate((0, 0, 0), (0, 0, 1), arm_tilt)
        seg = seg.union(arm)

    seg = seg.cut(
        cq.Workplane("XY").center(HOLE_R_POS, 0).circle(HOLE_D / 2).extrude(THK + 2, both=True)
    )
    return seg.val()


plain = make_segment(None)
cache = {}
solids = []
for i in range(N_SEG):
    ang = i * SEG_PITCH + SEG_PHASE
    if i in ARM_SEG_IDX:
        # arm direction: nearest of 90+-splay / 270+-splay
        cands = [90 - ARM_SPLAY, 90 + ARM_SPLAY, 270 - ARM_SPLAY, 270 + ARM_SPLAY]
        arm_dir = min(cands, key=lambda c: abs(c - ang))
        tilt = round(arm_dir - ang, 6)
        if tilt not in cache:
            cache[tilt] = make_segment(tilt)
        base = cache[tilt]
    else:
        base = plain
    solids.append(base.rotate((0, 0, 0), (0, 0, 1), ang))

result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(solids)])
